import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 31.4            # overall height
FLOOR = 8.5         # pocket floor height
Y_FRONT = -22.45    # front apex of the lens outline (bore centre at origin)
R_BACK = 54.45      # back (large) arc radius
BACK_CY = Y_FRONT - 10.1   # back arc centre lies in front of the part
R_FRONT = 145.0     # front (shallow) arc radius
FRONT_CY = Y_FRONT + R_FRONT
CORNER_R = 4.0      # rounding of the two lens tips

# pocket (three lobes, open to the front)
LOBE_R = 14.0
LOBE_X = 20.3
LOBE_Y = -12.6
CEN_R = 11.2
CUSP_R = 3.0
FLOOR_FILLET = 1.3
WALL_FRONT_R = 3.5
FLOOR_CHAMFER = 1.4

# central blind bore with a shallow recess in its bottom
BORE_R = CEN_R - 0.15
BORE_CH = 0.8
BORE_DEPTH = 7.0
RECESS_R = 8.8
RECESS_DEPTH = 0.4

# through holes on raised conical bosses (pocket floor)
BOSS_R0 = 6.0
BOSS_R1 = 4.65
BOSS_H = 1.2
CB_HOLE_R = 3.5
CB_TOP_CH = 0.3        # small chamfer on the hole at the boss top
CB_BOT_CB_R = 6.4       # counterbore from below
CB_BOT_CB_D = 5.0       # depth of the full-diameter part (drill point above)

# flange holes (two mirrored pairs) in the raised rim
FL_POS = ((18.8, 11.65), (41.7, -10.8))
FL_HOLE_R = 2.4
FL_CHAMFER = 0.7
FL_BOT_CB_R = 4.4       # counterbore from below
FL_BOT_CB_D = 6.0
DRILL_POINT = 118.0     # included angle of the drill point ending the counterbores

EDGE_R = 1.0            # rounding of outer top / bottom edges
RIM_R = 0.7             # rounding of the pocket rim
HOLE_BOT_CH = 0.5

# ---------------- outer body: intersection of two discs ----------------
back = cq.Workplane("XY").center(0, BACK_CY).circle(R_BACK).extrude(H)
front = cq.Workplane("XY").center(0, FRONT_CY).circle(R_FRONT).extrude(H)
body = back.intersect(front)
body = body.edges("|Z").fillet(CORNER_R)
body = body.faces("<Z").edges().fillet(EDGE_R)
body = body.faces(">Z").edges().fillet(EDGE_R)


# ---------------- 2D helpers ----------------
def _unit(vx, vy):
    n = math.hypot(vx, vy)
    return vx / n, vy / n


def _ext_tangent_center(c1, r1, c0, r0, r):
    """centre of circle radius r externally tangent to both circles (upper one)"""
    d1 = r1 + r
    d0 = r0 + r
    dx, dy = c0[0] - c1[0], c0[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (d1 * d1 - d0 * d0 + d * d) / (2 * d)
    h = math.sqrt(max(d1 * d1 - a * a, 0.0))
    ux, uy = dx / d, dy / d
    px, py = c1[0] + a * ux, c1[1] + a * uy
    s1 = (px - h * uy, py + h * ux)
    s2 = (px + h * uy, py - h * ux)
    return s1 if s1[1] > s2[1] else s2


def _tp(c, r, f):
    ux, uy = _unit(f[0] - c[0], f[1] - c[1])
    return (c[0] + r * ux, c[1] + r * uy)


def _arc_mid(c, r, p, q, cw=True):
    a1 = math.atan2(p[1] - c[1], p[0] - c[0])
    a2 = math.atan2(q[1] - c[1], q[0] - c[0])
    if cw:
        while a2 > a1:
            a2 -= 2 * math.pi
    else:
        while a2 < a1:
            a2 += 2 * math.pi
    am = 0.5 * (a1 + a2)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def _short_mid(c, r, p, q):
    ux, uy = _unit((p[0] + q[0]) / 2 - c[0], (p[1] + q[1]) / 2 - c[1])
    return (c[0] + r * ux, c[1] + r * uy)


# ---------------- pocket profile ----------------
cL = (-LOBE_X, LOBE_Y)
cR = (LOBE_X, LOBE_Y)
c0 = (0.0, 0.0)
XP = LOBE_X + LOBE_R

fL = _ext_tangent_center(cL, LOBE_R, c0, CEN_R, CUSP_R)
fR = _ext_tangent_center(cR, LOBE_R, c0, CEN_R, CUSP_R)
tL1 = _tp(cL, LOBE_R, fL)
tL0 = _tp(c0, CEN_R, fL)
tR0 = _tp(c0, CEN_R, fR)
tR1 = _tp(cR, LOBE_R, fR)

# rounding of the front-inner corners of the end walls (built into the tool)
_yc = FRONT_CY - math.sqrt((R_FRONT - WALL_FRONT_R) ** 2 - (XP + WALL_FRONT_R) ** 2)
wcR = (XP + WALL_FRONT_R, _yc)
wcL = (-XP - WALL_FRONT_R, _yc)
wsR = (XP, _yc)
wsL = (-XP, _yc)
_nR = _unit(wcR[0], wcR[1] - FRONT_CY)
_nL = _unit(wcL[0], wcL[1] - FRONT_CY)
wfR = (R_FRONT * _nR[0], FRONT_CY + R_FRONT * _nR[1])
wfL = (R_FRONT * _nL[0], FRONT_CY + R_FRONT * _nL[1])
woR = (wfR[0] + 3 * _nR[0], wfR[1] + 3 * _nR[1])
woL = (wfL[0] + 3 * _nL[0], wfL[1] + 3 * _nL[1])
Y_OUT = Y_FRONT - 8.0

p_l = (-XP, LOBE_Y)
p_r = (XP, LOBE_Y)


def pocket_profile(z):
    return (
        cq.Workplane("XY").workplane(offset=z)
        .moveTo(woL[0], Y_OUT)
        .lineTo(*woL)
        .lineTo(*wfL)
        .threePointArc(_short_mid(wcL, WALL_FRONT_R, wfL, wsL), wsL)
        .lineTo(*p_l)
        .threePointArc(_arc_mid(cL, LOBE_R, p_l, tL1, cw=True), tL1)
        .threePointArc(_short_mid(fL, CUSP_R, tL1, tL0), tL0)
        .threePointArc(_arc_mid(c0, CEN_R, tL0, tR0, cw=True), tR0)
        .threePointArc(_short_mid(fR, CUSP_R, tR0, tR1), tR1)
        .threePointArc(_arc_mid(cR, LOBE_R, tR1, p_r, cw=True), p_r)
        .lineTo(*wsR)
        .threePointArc(_short_mid(wcR, WALL_FRONT_R, wsR, wfR), wfR)
        .lineTo(*woR)
        .lineTo(woR[0], Y_OUT)
        .close()
    )


# pocket cutter with rounded bottom edges -> floor-to-wall fillet
tool = pocket_profile(FLOOR).extrude(H)
tool = tool.faces("<Z").edges().fillet(FLOOR_FILLET)

# 45 deg chamfer along the open front edge of the floor (conical, follows front arc)
_z0 = FLOOR - FLOOR_CHAMFER - 1.0
_ring = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(R_FRONT + 5, FLOOR + 1 - _z0, cq.Vector(0, FRONT_CY, _z0)))
_ring = _ring.cut(cq.Workplane("XY").add(
    cq.Solid.makeCone(R_FRONT + 1, R_FRONT - FLOOR_CHAMFER, FLOOR - _z0,
                      cq.Vector(0, FRONT_CY, _z0))))
_ring = _ring.cut(cq.Workplane("XY").add(
    cq.Solid.makeCylinder(R_FRONT - FLOOR_CHAMFER, 3, cq.Vector(0, FRONT_CY, FLOOR - 0.001))))
_foot = pocket_profile(_z0 - 1).extrude(FLOOR + 2 - _z0)
tool = tool.union(_ring.intersect(_foot))

body = body.cut(tool)
# round the rim of the pocket (top-face edges that are not on the outer boundary)
body = body.faces(">Z").edges().filter(
    lambda e: e.Center().y > Y_FRONT + 3.0 and e.Center().x ** 2 + (e.Center().y - BACK_CY) ** 2 < (R_BACK - 3.0) ** 2
).fillet(RIM_R)

# ---------------- central blind bore ----------------
body = body.cut(
    cq.Workplane("XY").workplane(offset=FLOOR - BORE_DEPTH).circle(BORE_R).extrude(BORE_DEPTH + 3)
)
# chamfer on the bore rim where it meets the floor (front part only)
_bch = cq.Workplane("XY").add(cq.Solid.makeCone(
    BORE_R - 0.5, BORE_R + BORE_CH + 0.01, BORE_CH + 0.5, cq.Vector(0, 0, FLOOR - BORE_CH - 0.5)))
_bch = _bch.intersect(cq.Workplane("XY").box(4 * BORE_R, 2 * BORE_R, 10, centered=(True, False, True))
                      .translate((0, -2 * BORE_R, FLOOR)))
body = body.cut(_bch)
body = body.cut(
    cq.Workplane("XY").workplane(offset=FLOOR - BORE_DEPTH - RECESS_DEPTH)
    .circle(RECESS_R).extrude(RECESS_DEPTH + 0.5)
)

# ---------------- raised conical bosses ----------------
for sx in (-1, 1):
    boss = cq.Solid.makeCone(BOSS_R0, BOSS_R1, BOSS_H, cq.Vector(sx * LOBE_X, LOBE_Y, FLOOR - 0.01))
    body = body.union(cq.Workplane("XY").add(boss))


# ---------------- holes ----------------
def _hole_cutter(x, y, r, z_top, ch_top, cb_r, cb_d, ch_bot):
    s = cq.Solid.makeCylinder(r, z_top + 2, cq.Vector(x, y, -1))
    if ch_top > 0:
        s = s.fuse(cq.Solid.makeCone(r, r + ch_top + 1, ch_top + 1,
                                     cq.Vector(x, y, z_top - ch_top)))
    s = s.fuse(cq.Solid.makeCylinder(cb_r, cb_d + 1, cq.Vector(x, y, -1)))
    tip_h = cb_r / math.tan(math.radians(DRILL_POINT / 2))
    s = s.fuse(cq.Solid.makeCone(cb_r, 0.0, tip_h, cq.Vector(x, y, cb_d)))
    s = s.fuse(cq.Solid.makeCone(cb_r + ch_bot + 1, cb_r, ch_bot + 1, cq.Vector(x, y, -1)))
    return s


for sx in (-1, 1):
    body = body.cut(cq.Workplane("XY").add(
        _hole_cutter(sx * LOBE_X, LOBE_Y, CB_HOLE_R, FLOOR + BOSS_H, CB_TOP_CH,
                     CB_BOT_CB_R, CB_BOT_CB_D, HOLE_BOT_CH)))

for (hx, hy) in FL_POS:
    for sx in (-1, 1):
        x, y = sx * hx, hy
        body = body.cut(cq.Workplane("XY").add(
            _hole_cutter(x, y, FL_HOLE_R, H, FL_CHAMFER,
                         FL_BOT_CB_R, FL_BOT_CB_D, HOLE_BOT_CH)))

result = body
